import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Mercury-style capsule with launch-escape tower.
# Axis of revolution = Y.  Heat-shield (wide, open) end at Y = 0, the tower
# points to -Y.  Everything is finally clocked about Y by CLOCK degrees.
# Angles "theta" are measured around Y from +X toward +Z (theta=90 is the top).
# ---------------------------------------------------------------------------

# --- capsule -----------------------------------------------------------------
R_BASE = 40.5          # radius of the wide (open) end
SLOPE = 0.565          # dr/dy of the conical body (half angle ~29.5 deg)
Y_NECK = -50.0         # where the cone runs into the rounded nose
Y_NOSE = -57.0         # tip of the rounded nose
Y_SEAM = -31.0         # seam between body and neck section
WALL = 4.6             # shell wall thickness (open end)
Y_FLOOR = -34.0        # depth of the inner cavity

# --- escape tower ------------------------------------------------------------
Y_NOZ_BASE = -90.8     # flat back face of the motor nozzle cone
Y_NOZ_TIP = -106.0     # narrow end of the motor cone (joins the rod)
R_NOZ_BASE = 12.6
R_NOZ_TIP = 4.9
R_ROD = 4.45           # escape motor / rod radius
Y_ROD_TIP_START = -223.5
Y_TIP = -237.0
TIP_SPHERE_R = 1.35
TRUSS_R = 11.0         # radial position of the four longerons
LONGERON_R = 1.4
BRACE_R = 0.6
NOZ_R_POS = 9.6        # radial position of the nozzle throats
NOZ_THROAT_R = 1.5
NOZ_EXIT_R = 3.7
NOZ_LEN = 6.0
NOZ_CANT = 32.0        # outward cant of the small nozzles

Y_MID = -62.5          # middle frame of the escape-tower truss

# --- details -----------------------------------------------------------------
GROOVE_W = 0.6         # width of the panel grooves
NOTCH_W = 8.0          # slot through the rim at the bottom
NOTCH_D = 14.0         # depth of that slot along the axis
NOTCH_FRAME_W = 14.0   # U frame around the slot

CLOCK = -7.0           # clocking of the whole assembly about Y


def cone_r(y):
    return R_BASE + SLOPE * y


K = math.sqrt(1.0 + SLOPE * SLOPE)


def surf_plane(theta, y, lift=0.0):
    """Plane tangent to the cone at angle theta (deg) and axial position y.
    local x = circumferential, local y = up the generatrix (toward the rim),
    local z = outward normal."""
    t = math.radians(theta)
    r = cone_r(y)
    c, s = math.cos(t), math.sin(t)
    n = cq.Vector(c / K, -SLOPE / K, s / K)
    p = cq.Vector(r * c, y, r * s) + n * lift
    xd = cq.Vector(s, 0.0, -c)
    return cq.Plane(origin=p, xDir=xd, normal=n)


def surf_box(theta, y, w, l, h, sink=1.0, rot=0.0, lift=0.0):
    """Box on the cone surface: width w (circumferential), length l (along the
    generatrix), height h above the surface, sunk 'sink' below it."""
    pl = surf_plane(theta, y, lift)
    return (cq.Workplane(pl).workplane(offset=-sink)
            .transformed(rotate=(0, 0, rot)).rect(w, l).extrude(h + sink))


def surf_cyl(theta, y, rad, h, sink=1.0, lift=0.0):
    pl = surf_plane(theta, y, lift)
    return cq.Workplane(pl).workplane(offset=-sink).circle(rad).extrude(h + sink)


def surf_ring(theta, y, ro, ri, h, sink=1.0, lift=0.0):
    pl = surf_plane(theta, y, lift)
    return (cq.Workplane(pl).workplane(offset=-sink).circle(ro).circle(ri)
            .extrude(h + sink))


def patch(y1, y2, th1, th2, h, base=0.0, h1=None):
    """Conformal raised patch on the cone between y1..y2 and th1..th2,
    from 'base' up to 'h' above the nominal cone surface ('h1' = height at
    the y1 end if the patch is tapered)."""
    dk, bk = h * K, base * K
    dk1 = dk if h1 is None else h1 * K
    pts = [(cone_r(y1) + bk - 0.05, y1), (cone_r(y2) + bk - 0.05, y2),
           (cone_r(y2) + dk, y2), (cone_r(y1) + dk1, y1)]
    sol = (cq.Workplane("XY").polyline(pts).close()
           .revolve(th2 - th1, (0, 0, 0), (0, -1, 0)))
    return sol.rotate((0, 0, 0), (0, -1, 0), th1)


# =============================================================================
# capsule body (filled first, cavity cut afterwards)
# =============================================================================
r_neck = cone_r(Y_NECK)
body = (cq.Workplane("XY")
        .moveTo(0, Y_NOSE)
        .threePointArc((r_neck * 0.55, Y_NOSE + 1.6), (r_neck, Y_NECK))
        .lineTo(R_BASE, 0)
        .lineTo(0, 0)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 1, 0), 90))      # put the revolve seam underneath

adds = []
# ---- top: raised hatch sector and plateau -----------------------------------
TOP_H = 0.45
adds.append(patch(-31.0, -0.3, 23.0, 161.0, TOP_H))                 # top sector
adds.append(patch(-40.0, -31.0, 23.0, 161.0, TOP_H, h1=0.02))       # its taper
PLAT_H = 1.5
adds.append(patch(-28.5, -10.5, 72.0, 122.0, PLAT_H))        # hatch plateau
adds.append(patch(-31.0, -28.5, 72.0, 122.0, PLAT_H, h1=TOP_H))  # plateau ramp
adds.append(patch(-28.5, -15.0, 76.0, 114.0, PLAT_H + 0.35))  # instrument panel
adds.append(surf_box(106.0, -23.5, 3.0, 10.0, 1.4, sink=1.0, rot=-8, lift=PLAT_H))  # block
adds.append(surf_box(103.5, -17.0, 5.0, 2.4, 1.9, sink=1.0, lift=PLAT_H))           # block cap
adds.append(surf_cyl(91.0, -23.0, 2.3, 1.2, sink=1.0, lift=PLAT_H + 0.35))         # screw head
# ribs near the rim on top
for th in (101.0, 105.0, 109.0):
    adds.append(surf_box(th, -6.0, 1.5, 9.0, 1.2, sink=1.0, lift=TOP_H))
for th in (68.0, 73.5, 79.0):
    adds.append(surf_box(th, -6.0, 2.6, 9.0, 0.6, sink=1.0, lift=TOP_H))
# window panel on the upper +X side
adds.append(patch(-32.0, -12.5, 46.0, 71.0, 1.5))
adds.append(surf_ring(57.0, -28.0, 3.8, 3.0, 1.0, sink=1.0, lift=1.5))   # window ring
adds.append(surf_cyl(57.0, -28.0, 3.0, 0.5, sink=1.0, lift=1.5))        # window glass
# periscope door and small triangle on the upper -X side
PERI_W, PERI_L, PERI_T, PERI_OPEN = 6.5, 20.0, 0.9, 22.0
_pp = surf_plane(123.0, -18.0)
adds.append(cq.Workplane(_pp)
            .transformed(offset=(PERI_W / 2.0, 0, -0.6), rotate=(0, PERI_OPEN, 6))
            .center(-PERI_W / 2.0, 0).rect(PERI_W, PERI_L).extrude(PERI_T))      # periscope door
adds.append(surf_box(123.0, -18.0, PERI_W, PERI_L, 0.5, sink=1.0, rot=6))          # door frame
_tp = surf_plane(113.5, -27.5)
adds.append(cq.Workplane(_tp).workplane(offset=-1.0)
            .polyline([(-2.2, -5.0), (2.2, -5.0), (0.3, 5.0)]).close()
            .extrude(1.0 + 1.3))
# square panels on the flanks
adds.append(patch(-21.5, -12.5, 27.0, 43.0, TOP_H + 0.35))
adds.append(patch(-20.5, -11.5, 141.0, 157.0, TOP_H + 0.35))
# bolt pairs ("8" marks) -- two small ring heads side by side circumferentially
BOLT_R = 1.55
for th, yy, lf in ((1.0, -5.5, 0.0), (45.0, -6.5, 0.0), (138.5, -4.4, 0.0),
                   (179.5, -2.8, 0.0), (90.5, -5.5, TOP_H), (93.0, -34.5, TOP_H)):
    r = cone_r(yy)
    dth = math.degrees(BOLT_R / r)
    for d in (-dth, dth):
        adds.append(surf_ring(th + d, yy, BOLT_R, BOLT_R * 0.55, 0.55, sink=0.6, lift=lf))
# bottom: box and stem
adds.append(surf_box(-90.0, -26.5, 13.0, 5.5, 0.7, sink=1.0))
adds.append(surf_box(-90.0, -18.8, 2.2, 9.0, 0.7, sink=1.0))
# notch frame (outside)
adds.append(surf_box(-90.0, -(NOTCH_D + 2.6) / 2.0, NOTCH_FRAME_W, (NOTCH_D + 2.6) * K * 0.88,
                     0.8, sink=1.0))

for a in adds:
    body = body.union(a)

# ---- cavity (open wide end) -------------------------------------------------
wk = WALL * K
cavity = (cq.Workplane("XY")
          .moveTo(0, Y_FLOOR)
          .lineTo(cone_r(Y_FLOOR) - wk, Y_FLOOR)
          .lineTo(R_BASE - wk, 0)
          .lineTo(R_BASE - wk, 5)
          .lineTo(0, 5)
          .close()
          .revolve(360, (0, 0, 0), (0, 1, 0))
          .rotate((0, 0, 0), (0, 1, 0), 90))
body = body.cut(cavity)

# inner U frame around the notch
inner = surf_box(-90.0, -8.0, NOTCH_FRAME_W, 16.0, 0.0, sink=WALL + 1.2)
inner = inner.intersect(
    cq.Workplane("XY").add(cq.Solid.makeBox(200, 100, 200, cq.Vector(-100, -100, -100))))
body = body.union(inner)

# ---- cuts: seam groove, radial grooves, recessed panels, notch ----------------
body = body.cut(patch(Y_SEAM - 0.3, Y_SEAM + 0.3, 161.0, 383.0, 3.0, base=-0.35))

for th, y1, y2 in ((23.0, Y_SEAM + 0.5, -0.4), (-34.0, Y_SEAM + 0.5, -0.4),
                   (161.0, Y_SEAM + 0.5, -0.4), (212.0, Y_SEAM + 0.5, -0.4),
                   (194.0, Y_SEAM + 0.5, -21.5)):
    g = surf_box(th, (y1 + y2) / 2.0, GROOVE_W, (y2 - y1) * K, 3.0, sink=0.35)
    body = body.cut(g)

# slot across the screw head
body = body.cut(surf_box(91.0, -23.0, 0.6, 4.0, 3.0, sink=-(PLAT_H + 1.2), rot=35))

# notch through the rim at the bottom
notch = surf_box(-90.0, -NOTCH_D / 2.0 + 2.0, NOTCH_W, NOTCH_D * K + 2.0, 8.0, sink=8.0)
body = body.cut(notch)

# =============================================================================
# escape tower
# =============================================================================
# rounded tip: a sphere (centre on the axis) tangent to the tip cone


def _tip_y(beta):
    return (Y_ROD_TIP_START - (R_ROD - TIP_SPHERE_R * math.cos(beta)) / math.tan(beta)
            + TIP_SPHERE_R * math.sin(beta) - TIP_SPHERE_R)


_lo, _hi = math.radians(3.0), math.radians(60.0)
for _ in range(80):
    _mid = 0.5 * (_lo + _hi)
    if _tip_y(_mid) < Y_TIP:
        _lo = _mid
    else:
        _hi = _mid
TIP_BETA = 0.5 * (_lo + _hi)
_yc = Y_TIP + TIP_SPHERE_R
tip_tan = (TIP_SPHERE_R * math.cos(TIP_BETA), _yc - TIP_SPHERE_R * math.sin(TIP_BETA))
_psi = 0.5 * (math.pi / 2 - TIP_BETA)
tip_mid = (TIP_SPHERE_R * math.sin(_psi), _yc - TIP_SPHERE_R * math.cos(_psi))

tower = (cq.Workplane("XY")
         .moveTo(0, Y_NOZ_BASE)
         .lineTo(R_NOZ_BASE, Y_NOZ_BASE)
         .lineTo(R_NOZ_TIP, Y_NOZ_TIP)
         .lineTo(R_ROD + 0.3, Y_NOZ_TIP)
         .threePointArc((R_ROD + 0.75, Y_NOZ_TIP - 0.9), (R_ROD + 0.3, Y_NOZ_TIP - 1.8))
         .lineTo(R_ROD, Y_NOZ_TIP - 1.8)
         .lineTo(R_ROD, Y_ROD_TIP_START)
         .lineTo(*tip_tan)
         .threePointArc(tip_mid, (0, Y_TIP))
         .close()
         .revolve(360, (0, 0, 0), (0, 1, 0))
         .rotate((0, 0, 0), (0, 1, 0), 90))
# soften the rim of the motor cone base
tower = tower.edges(cq.selectors.NearestToPointSelector((0, Y_NOZ_BASE, R_NOZ_BASE))).fillet(0.7)

# four canted bell nozzles on the back face of the motor cone
for i in range(4):
    th = math.radians(90 * i)
    c, s = math.cos(th), math.sin(th)
    base = cq.Vector(NOZ_R_POS * c, Y_NOZ_BASE - 0.6, NOZ_R_POS * s)
    ca = math.radians(NOZ_CANT)
    d = cq.Vector(math.sin(ca) * c, math.cos(ca), math.sin(ca) * s)
    noz = cq.Workplane("XY").add(cq.Solid.makeCone(NOZ_THROAT_R, NOZ_EXIT_R, NOZ_LEN, base, d))
    # hollow bell: conical recess in the exit
    rec_start = base + d * (NOZ_LEN * 0.35)
    rec = cq.Solid.makeCone(0.6, NOZ_EXIT_R - 0.45, NOZ_LEN * 0.65 + 0.01, rec_start, d)
    noz = noz.cut(cq.Workplane("XY").add(rec))
    tower = tower.union(noz)


def rod(p1, p2, r):
    v1, v2 = cq.Vector(*p1), cq.Vector(*p2)
    d = v2 - v1
    return cq.Workplane("XY").add(cq.Solid.makeCylinder(r, d.Length, v1, d.normalized()))


# truss
Y_T0 = Y_NOZ_BASE - 0.1
Y_T1 = (TRUSS_R - R_BASE) / SLOPE + 1.5     # longerons end inside the capsule wall
corner = []
for i in range(4):
    th = math.radians(45 + 90 * i)
    corner.append((TRUSS_R * math.cos(th), TRUSS_R * math.sin(th)))

members = []
for (x, z) in corner:
    members.append(rod((x, Y_T0, z), (x, Y_T1, z), LONGERON_R))
yb0, yb1 = Y_NOZ_BASE + 4.0, (TRUSS_R - R_BASE) / SLOPE - 0.5
for i in range(4):
    (x1, z1), (x2, z2) = corner[i], corner[(i + 1) % 4]
    # transverse frames
    for yy in (Y_NOZ_BASE + 1.0, yb0, Y_MID, yb1):
        members.append(rod((x1, yy, z1), (x2, yy, z2), BRACE_R))
    # X bracing in the lower bay, N bracing in the upper bay
    members.append(rod((x1, yb0, z1), (x2, Y_MID, z2), BRACE_R))
    members.append(rod((x2, yb0, z2), (x1, Y_MID, z1), BRACE_R))
    members.append(rod((x1, Y_MID, z1), (x2, yb1, z2), BRACE_R))

# thin gusset plates filling the bow-tie triangles of the X bracing
GUSSET_T = 0.35
for i in range(4):
    (x1, z1), (x2, z2) = corner[i], corner[(i + 1) % 4]
    p1a, p2a = cq.Vector(x1, yb0, z1), cq.Vector(x2, yb0, z2)
    p1b, p2b = cq.Vector(x1, Y_MID, z1), cq.Vector(x2, Y_MID, z2)
    ctr = (p1a + p2a + p1b + p2b) * 0.25
    face_n = cq.Vector((x1 + x2) / 2.0, 0, (z1 + z2) / 2.0).normalized()
    for (pa, pb) in ((p1a, p2a), (p1b, p2b)):
        xd = (pb - pa).normalized()
        gpl = cq.Plane(origin=ctr - face_n * (GUSSET_T / 2.0), xDir=xd, normal=face_n)
        pts = [gpl.toLocalCoords(v) for v in (pa, pb, ctr)]
        members.append(cq.Workplane(gpl).polyline([(v.x, v.y) for v in pts]).close()
                       .extrude(GUSSET_T))

for m in members:
    tower = tower.union(m)

# V-shaped foot fins where the longerons land on the capsule: two tapered
# triangular fins standing normal to the cone surface
y_land = (TRUSS_R - R_BASE) / SLOPE
FIN_L = 7.5
FIN_H = 2.2
FIN_SPREAD = 10.0
FIN_T = 0.5
for (x, z) in corner:
    th = math.degrees(math.atan2(z, x))
    pl0 = surf_plane(th, y_land)
    lx, ly, lz = pl0.xDir, pl0.yDir, pl0.zDir
    for sgn in (-1.0, 1.0):
        a = math.radians(FIN_SPREAD * sgn)
        along = ly * math.cos(a) + lx * math.sin(a)
        side = lx * math.cos(a) - ly * math.sin(a)
        fpl = cq.Plane(origin=pl0.origin + along * 0.3 - side * (FIN_T / 2),
                       xDir=along, normal=side)
        fin = (cq.Workplane(fpl)
               .polyline([(0, -0.8), (FIN_L, -0.8), (FIN_L, 0.25), (0, FIN_H)])
               .close().extrude(FIN_T))
        tower = tower.union(fin)
    # web plate filling the V
    hw = math.tan(math.radians(FIN_SPREAD)) * FIN_L
    web = (cq.Workplane(pl0).workplane(offset=-0.6)
           .polyline([(-0.6, 0.0), (0.6, 0.0), (hw, FIN_L * 0.95), (-hw, FIN_L * 0.95)])
           .close().extrude(1.2))
    tower = tower.union(web)

result = body.union(tower)
result = result.rotate((0, 0, 0), (0, 1, 0), CLOCK)

VIEW = {"azimuth": 45, "elevation": 26}
